import cadquery as cq
import math

# =====================================================================
#  Conical hood with flat mounting floor, slotted neck and cross bar.
#  Built in a local frame:  X = u (along the mounting bar),
#  Y = cone axis (front face at y = 0, growing to the back),
#  Z = w (normal of the mounting floor).  Finally rotated about Y by TILT.
# =====================================================================
TILT = 29.0            # tilt of floor / bar about the cone axis (deg)

# ---- cone ----
R_FRONT = 51.0         # outer radius at the front face (y = 0)
R_RIM = 97.0           # outer radius at the rim edge
Y_RIM = 82.0           # y of the outer rim edge
TAN_A = (R_RIM - R_FRONT) / Y_RIM          # tangent of cone half angle
COS_A = 1.0 / math.sqrt(1.0 + TAN_A ** 2)
WALL = 35.0            # cone wall thickness (perpendicular to the cone surface)
T_SIDE = 44.0          # thickness of the flat side walls at floor level
CAV_Y0 = 12.0          # front wall thickness (cavity starts here)
PHI_T = math.radians(6.0)    # side faces leave the rim circle here (back)
PHI_F = math.radians(-18.0)  # side faces leave the front circle here

# ---- floor / plate ----
W_TOP = -56.0          # floor top (= bar / neck top)
W_BOT = -77.0          # floor bottom
Y_BACK = 99.0          # back edge of the floor
NOSE_R = 57.0          # radius of the rounded nose
NOSE_WT = -20.0        # nose tangent line on the front face (w)

# ---- neck / bar ----
SLOT_GAP = 30.6
BAR_W = 31.6
BAR_HALF = 112.0
NECK_HALF = 48.0       # centre of the slot's round end (|u|)
Y_BAR0 = Y_BACK + SLOT_GAP
Y_BAR1 = Y_BAR0 + BAR_W
W_MID = 0.5 * (W_TOP + W_BOT)
END_HOLE_Y = 9.5       # end holes: distance from the bar's front face
BAR_HOLE_D = 6.5       # cross holes / end holes / long through hole
BAR_HOLE_U = 67.0      # cross holes at u = -BAR_HOLE_U, 0, +BAR_HOLE_U

# ---- front face details ----
RING_R, RING_D, RING_DEPTH = 43.0, 5.5, 8.0
SCAL_R, SCAL_D, SCAL_DEPTH = 24.3, 6.4, 8.0
HUB_R = 21.0           # hub cone base radius
HUB_APEX = -37.8       # hub cone apex (y)
HUB_CUT_W = -3.0       # hub is kept above this w
BOSS_Y0, BOSS_Y1 = -37.8, -11.5
SLOT_BL, SLOT_BR = -22.5, 22.0   # slot under the hub: u at the floor level
SLOT_TL, SLOT_TR = -14.0, 4.0    # ... and at the hub cut level
BOSS_C1 = (0.0, -2.0)   # (global X, global Z) of the small end centre
BOSS_R1 = 12.0
BOSS_C2 = (14.0, -17.5)
BOSS_R2 = 17.5
BOSS_HOLES = [(0.0, -2.0), (7.9, -17.5), (20.2, -17.5)]
BOSS_HOLE_D = 9.6

# ---- rim details ----
HEX_AF = 13.0          # hex pocket across flats
HEX_DEPTH = 6.0
HEX_HOLE_D = 4.5
SLIT_W, SLIT_D, SLIT_L = 5.0, 7.0, 22.0

SIN_T, COS_T = math.sin(math.radians(TILT)), math.cos(math.radians(TILT))


def g2l(X, Z):
    """global front-view coordinates (X right, Z up) -> local (u, w)"""
    return (X * COS_T + Z * SIN_T, -X * SIN_T + Z * COS_T)


def r_at(y):
    return R_FRONT + TAN_A * y


def u_side(y, r_off=0.0, w=W_TOP):
    """u where the flat side plane (tangent at PHI_T) reaches level w"""
    return (r_at(y) - r_off - w * math.sin(PHI_T)) / math.cos(PHI_T)


def tangent_angle(r, pu, pw, upper=True):
    """angle of the tangent point on circle r seen from the point (pu, pw)"""
    d = math.hypot(pu, pw)
    a = math.atan2(pw, pu)
    b = math.acos(r / d)
    return a + b if upper else a - b


def hull_wire(y, r, U, wt, wb, phi=PHI_T):
    """arc (radius r) between points at phi / pi-phi, flat sides
    down to (+-U, wt), vertical plate sides to wb and the floor line."""
    V = lambda u, w: cq.Vector(u, y, w)
    TR = V(r * math.cos(phi), r * math.sin(phi))
    TL = V(-r * math.cos(phi), r * math.sin(phi))
    e = [cq.Edge.makeThreePointArc(TR, V(0, r), TL), cq.Edge.makeLine(TL, V(-U, wt))]
    if wt - wb > 1e-6:
        e += [cq.Edge.makeLine(V(-U, wt), V(-U, wb)), cq.Edge.makeLine(V(-U, wb), V(U, wb)),
              cq.Edge.makeLine(V(U, wb), V(U, wt))]
    else:
        e += [cq.Edge.makeLine(V(-U, wt), V(U, wt))]
    e.append(cq.Edge.makeLine(V(U, wt), TR))
    return cq.Wire.assembleEdges(e)


def loft(y0, y1, r_off, wt, wb, phi0=PHI_T, phi1=PHI_T):
    w0 = hull_wire(y0, r_at(y0) - r_off, u_side(y0, r_off, wt), wt, wb, phi0)
    w1 = hull_wire(y1, r_at(y1) - r_off, u_side(y1, r_off, wt), wt, wb, phi1)
    return cq.Workplane().add(cq.Solid.makeLoft([w0, w1], True))


def nose_cutter(radius):
    """region in front of / below the nose arc (centre y=NOSE_R, w=NOSE_WT)"""
    cy, cw = NOSE_R, NOSE_WT
    a = math.radians(45)
    return (cq.Workplane("YZ").workplane(offset=-300)
            .moveTo(-60, W_BOT - 60).lineTo(cy, W_BOT - 60).lineTo(cy, cw - radius)
            .threePointArc((cy - radius * math.cos(a), cw - radius * math.sin(a)), (cy - radius, cw))
            .lineTo(-60, cw).close().extrude(600))


BIG = 1200.0


def half_space(p0, n):
    """solid {p : (p - p0) . n <= 0} (bounded by a large box)"""
    n = cq.Vector(n).normalized()
    x = n.cross(cq.Vector(0, 0, 1))
    if x.Length < 1e-6:
        x = cq.Vector(1, 0, 0)
    pl = cq.Plane(origin=cq.Vector(p0), xDir=x.normalized(), normal=n)
    return cq.Workplane(pl).rect(BIG, BIG).extrude(-BIG)


def cut_all(b, tools):
    """fuse the tool solids first, then subtract them in one boolean"""
    t = tools[0].fuse(*tools[1:]) if len(tools) > 1 else tools[0]
    return b.cut(cq.Workplane().add(t))


def drill(p, d, dia, depth, point=60.0):
    """blind drilled hole (cylinder + conical point) starting at p along d"""
    d = cq.Vector(d).normalized()
    cyl = cq.Solid.makeCylinder(dia / 2, depth, p, d)
    h = (dia / 2) / math.tan(math.radians(point / 2))
    tip = cq.Solid.makeCone(dia / 2, 0.0, h, p + d * depth, d)
    return cyl.fuse(tip)


def gpt(X, Z, y):
    u, w = g2l(X, Z)
    return cq.Vector(u, y, w)


def loc_ang(global_deg):
    return math.radians(global_deg - TILT)


# ---------------- outer body ----------------
body = loft(0.0, Y_RIM, 0.0, W_TOP, W_BOT, PHI_F, PHI_T).union(
    loft(Y_RIM, Y_BACK + 30.0, 0.0, W_TOP, W_BOT))
body = body.cut(cq.Workplane().box(600, 100, 600).translate((0, -50, 0)))       # front face y=0

# ---- back (rim) cut ----
# rim face: cone perpendicular to the generators through the rim edge; on the
# flat sides it continues as the planes tangent to that cone (they also form
# the chamfered back corners of the floor).
apex_y = Y_RIM + R_RIM * TAN_A
cone_keep = cq.Workplane().add(
    cq.Solid.makeCone(0, 800, 800 * TAN_A, pnt=cq.Vector(0, apex_y, 0), dir=cq.Vector(0, -1, 0)))
sin_a = TAN_A * COS_A
tang = {}
for s_ in (1, -1):
    c, sn = s_ * math.cos(PHI_T), math.sin(PHI_T)
    p0 = (R_RIM * c, Y_RIM, R_RIM * sn)
    g = (sin_a * c, COS_A, sin_a * sn)                 # generator direction
    tang[s_] = half_space(p0, g)
# below the tangent generators (the flat side regions) the tangent planes govern
sec_R = half_space((0, 0, 0), (-math.sin(PHI_T), 0, math.cos(PHI_T))).intersect(
    cq.Workplane().box(BIG, BIG, BIG).translate((BIG / 2, 0, 0)))
sec_L = sec_R.mirror("YZ")
keep_top = cone_keep.union(tang[1].intersect(sec_R)).union(tang[-1].intersect(sec_L))
keep_top = keep_top.intersect(cq.Workplane().box(BIG, BIG, BIG).translate((0, 0, W_TOP + BIG / 2)))
keep_bot = (tang[1].intersect(tang[-1])
            .intersect(cq.Workplane().box(BIG, BIG, BIG).translate((0, Y_BACK - BIG / 2, W_TOP - BIG / 2))))
body = body.intersect(keep_top.union(keep_bot))

# rounded nose
body = body.cut(nose_cutter(NOSE_R))

# ---------------- cavity ----------------
# thick conical wall on top (gives the wide rim face); the cavity profile is the
# hull of the inner circle and the inner floor corners; floor = plate top.


def cavity_wire(y):
    r = r_at(y) - WALL / COS_A
    U = u_side(y, 0.0, W_TOP) - T_SIDE / math.cos(PHI_T)
    tr = tangent_angle(r, U, W_TOP, True)
    V = lambda u, w: cq.Vector(u, y, w)
    TR = V(r * math.cos(tr), r * math.sin(tr))
    TL = V(-r * math.cos(tr), r * math.sin(tr))
    e = [cq.Edge.makeThreePointArc(TR, V(0, r), TL), cq.Edge.makeLine(TL, V(-U, W_TOP)),
         cq.Edge.makeLine(V(-U, W_TOP), V(U, W_TOP)), cq.Edge.makeLine(V(U, W_TOP), TR)]
    return cq.Wire.assembleEdges(e)


cav = cq.Workplane().add(cq.Solid.makeLoft([cavity_wire(CAV_Y0), cavity_wire(Y_BACK + 40.0)], True))
cav = cav.cut(nose_cutter(NOSE_R - 8.0))
body = body.cut(cav)

# ---------------- neck + bar ----------------
neck = (cq.Workplane("XY").workplane(offset=W_BOT).center(0, 0.5 * (Y_BACK + Y_BAR0))
        .rect(2 * NECK_HALF, SLOT_GAP + 2).extrude(W_TOP - W_BOT))
for s in (1, -1):
    neck = neck.cut(cq.Workplane("XY").workplane(offset=W_BOT - 1)
                    .center(s * NECK_HALF, 0.5 * (Y_BACK + Y_BAR0)).circle(SLOT_GAP / 2).extrude(40))
bar = (cq.Workplane("XY").workplane(offset=W_BOT).center(0, 0.5 * (Y_BAR0 + Y_BAR1))
       .rect(2 * BAR_HALF, BAR_W).extrude(W_TOP - W_BOT))
body = body.union(neck).union(bar)

for u in (-BAR_HOLE_U, BAR_HOLE_U):     # cross holes through the bar (along Y)
    body = body.cut(cq.Workplane("XZ").workplane(offset=-(Y_BAR1 + 5)).center(u, W_MID)
                    .circle(BAR_HOLE_D / 2).extrude(BAR_W + 10))
for s in (1, -1):                       # end holes
    body = body.cut(cq.Workplane("YZ").workplane(offset=s * (BAR_HALF + 1))
                    .center(Y_BAR0 + END_HOLE_Y, W_MID).circle(BAR_HOLE_D / 2).extrude(-16 * s))
# long hole along Y through nose, floor, neck and bar (the middle cross hole)
body = body.cut(cq.Workplane("XZ").workplane(offset=5).center(0, W_MID)
                .circle(BAR_HOLE_D / 2).extrude(-(Y_BAR1 + 10)))

# ---------------- front face details ----------------
# ring of holes in the front face (upper half, 20 deg pitch)
ring = [gpt(RING_R * math.cos(math.radians(a)), RING_R * math.sin(math.radians(a)), 0.0)
        for a in range(30, 211, 20)]
tools = [drill(p + cq.Vector(0, -1, 0), (0, 1, 0), RING_D, RING_DEPTH + 1) for p in ring]
# scallop holes around the hub base
for k in range(11):
    a = math.radians(18.0 * k)
    p = cq.Vector(SCAL_R * math.cos(a), -1.0, SCAL_R * math.sin(a))
    tools.append(drill(p, (0, 1, 0), SCAL_D, SCAL_DEPTH + 1))
body = cut_all(body, tools)

# slot through the nose below the hub (trapezoid in u-w, cut along y)
slot = (cq.Workplane("XZ").workplane(offset=10)
        .polyline([(SLOT_BL, W_TOP - 1.0), (SLOT_BR, W_TOP - 1.0), (SLOT_TR, HUB_CUT_W), (SLOT_TL, HUB_CUT_W)])
        .close().extrude(-(CAV_Y0 + 30.0)))
body = body.cut(slot, clean=False)

# hub: half cone standing on the front face
hub_len = -HUB_APEX
hub = cq.Workplane().add(cq.Solid.makeCone(HUB_R * (hub_len + 3) / hub_len, 0.0, hub_len + 3,
                                           pnt=cq.Vector(0, 3, 0), dir=cq.Vector(0, -1, 0)))
hub = hub.intersect(cq.Workplane().box(200, 200, 200).translate((0, 0, HUB_CUT_W + 100)))

# lever boss: hull of two circles, in front of the hub
c1 = g2l(*BOSS_C1)
c2 = g2l(*BOSS_C2)
dx, dz = c2[0] - c1[0], c2[1] - c1[1]
L = math.hypot(dx, dz)
ex, ez = dx / L, dz / L
nx, nz = -ez, ex
sb = (BOSS_R1 - BOSS_R2) / L            # external tangent geometry
cb = math.sqrt(1 - sb * sb)


def tp(c, r, side):
    # tangent point direction: rotate the normal towards the axis
    vx = sb * ex + side * cb * nx
    vz = sb * ez + side * cb * nz
    return (c[0] + r * vx, c[1] + r * vz)


p1a, p2a = tp(c1, BOSS_R1, 1), tp(c2, BOSS_R2, 1)
p1b, p2b = tp(c1, BOSS_R1, -1), tp(c2, BOSS_R2, -1)
far2 = (c2[0] + BOSS_R2 * ex, c2[1] + BOSS_R2 * ez)
far1 = (c1[0] - BOSS_R1 * ex, c1[1] - BOSS_R1 * ez)
boss = (cq.Workplane("XZ").workplane(offset=-BOSS_Y1)
        .moveTo(*p1a).lineTo(*p2a).threePointArc(far2, p2b).lineTo(*p1b).threePointArc(far1, p1a)
        .close().extrude(BOSS_Y1 - BOSS_Y0))
body = body.union(hub).union(boss)
hole_tools = []
for hx, hz in BOSS_HOLES:
    u, w = g2l(hx, hz)
    depth = 60.0 if (hx, hz) == BOSS_HOLES[0] else (BOSS_Y1 - BOSS_Y0) + 2
    hole_tools.append(cq.Solid.makeCylinder(BOSS_HOLE_D / 2, depth, cq.Vector(u, BOSS_Y0 - 1, w),
                                            cq.Vector(0, 1, 0)))
body = cut_all(body, hole_tools)

# ---------------- rim details ----------------
rim_tools = []
for k, a_g in enumerate(range(30, 211, 20)):
    g_ang = loc_ang(a_g)
    er = cq.Vector(math.cos(g_ang), 0, math.sin(g_ang))
    gdir = er * sin_a + cq.Vector(0, COS_A, 0)          # generator (out of rim face)
    base = er * R_RIM + cq.Vector(0, Y_RIM, 0)
    inward = er * (-COS_A) + cq.Vector(0, sin_a, 0)      # along rim face toward the axis
    # hex pocket
    hc = base + inward * 20.0
    et = cq.Vector(-math.sin(g_ang), 0, math.cos(g_ang))
    pl = cq.Plane(origin=hc + gdir * 1.0, xDir=et, normal=gdir)
    rim_tools.append(cq.Workplane(pl).polygon(6, HEX_AF / math.cos(math.pi / 6)).extrude(-(HEX_DEPTH + 1)).val())
    rim_tools.append(cq.Solid.makeCylinder(HEX_HOLE_D / 2, 24.0, hc + gdir * 1.0, gdir * -1.0))
    # small hole near the outer edge
    hs = base + inward * 7.5
    rim_tools.append(cq.Solid.makeCylinder(1.6, 10.0, hs + gdir * 1.0, gdir * -1.0))
body = cut_all(body, rim_tools)

# V slits cut into the outer cone surface at the rim
slit_tools = []
for a_g in range(40, 201, 20):
    g_ang = loc_ang(a_g)
    er = cq.Vector(math.cos(g_ang), 0, math.sin(g_ang))
    et = cq.Vector(-math.sin(g_ang), 0, math.cos(g_ang))
    ns = er * COS_A + cq.Vector(0, -sin_a, 0)           # outer surface normal
    base = er * R_RIM + cq.Vector(0, Y_RIM, 0)
    pl_out = cq.Plane(origin=base + ns * 2.0, xDir=et, normal=ns)
    pl_in = cq.Plane(origin=base - ns * SLIT_D, xDir=et, normal=ns)
    w_out = cq.Workplane(pl_out).polyline([(-SLIT_W / 2, -4), (SLIT_W / 2, -4), (0, SLIT_L)]).close().wires().val()
    w_in = cq.Workplane(pl_in).polyline([(-0.3, -4), (0.3, -4), (0, 3.0)]).close().wires().val()
    slit_tools.append(cq.Solid.makeLoft([w_out, w_in], True))
body = cut_all(body, slit_tools)

result = body.rotate((0, 0, 0), (0, 1, 0), -TILT)
